import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
W = 30.0          # overall width (X)
L = 65.0          # overall length (Y)
H = 35.0          # overall height (Z)

NARROW_X0 = 15.0  # channel part spans X in [NARROW_X0, W]
WIDE_Y0 = 42.3    # pipe-clamp block spans Y in [WIDE_Y0, L]

WEB_T = 3.0       # channel web thickness (at +X)
LIP_T = 9.5       # thickness of the end-cap lips (top / bottom)
CAP_L = 5.4       # length of the end-cap construction block along Y
CAP_BACK = 3.0    # cap back face position (Y) between tip round and web
CAP_BACK_TIP = 4.8  # cap back face position at the lip tips
CAP_BACK_X = 19.5 # where the concave plan round of the cap back ends
CAP_BLEND_TIP_R = 5.0  # concave blend cap -> thin flange at the lip tips
FLANGE_T = 4.5    # thin flange thickness behind the cap
CAP_BLEND_R = 1.0 # concave blend cap -> thin flange away from the tips
LIP_BLEND_R = 0.0 # tapering round on the lip tips at the -Y end (-> 0 at CAP_L)
END_BLEND_R = 5.3 # tapering round on the -Y end top/bottom edges (-> 0 at web)
BLEND_END_R = 0.3
TIP_BLEND_R = 0.0 # round on the vertical lip-tip edges at the -Y end

NOTCH_R = 10.0    # vertical pipe notch at +Y end
STRAP_RI = 14.8   # strap channel inner radius (around the notch axis)
WIN_Y0 = 52.0     # strap windows start (defines outer radius)
WIN_Z0 = 10.0
WIN_Z1 = 25.0
STRAP_SKIN = 0.2  # skin left at +Y end face

HOLE_D = 2.7
HOLE_Y = (6.6, 37.2)
HOLE_Z_OFF = 6.6  # from top / bottom face

CORNER_RX = 5.5   # elliptical vertical round on the block's (-X,-Y) corner
CORNER_RY = 9.9
CORNER_END_ANG = 266  # slight kink so the edge round stops at the -Y face
EDGE_R = 2.0      # rounds along the block's -X top/bottom edges

NUB_R = 5.2       # snap nubs on top / bottom (C-shaped clip beads)
NUB_RISE = 2.0    # height above the top / bottom face
NUB_Y0 = 7.4
NUB_Y1 = 17.2
NUB_X = 15.1      # axis position in X
NUB_HANG = 1.5    # how far the bead hangs below the face on the -X side
NUB_SLOT_X0 = 13.0  # slot under the overhang, between bead and lip tip
NUB_END_R = 2.2   # round on the bead ends
NUB_REACH = 4.2   # how far the bead overhangs the lip tip towards -X
NUB_BASE_R = 1.0  # blend between bead and face

TAB_DEPTH = 19.7
TAB_T = 2.0
ROD_R = 1.7
TAB_P0 = (27.95, 8.1)   # rod axis (x, y)
TAB_P1 = (18.5, 29.0)  # far edge of tab web (x, y)
TAB_CORNER_R = 1.5
TAB_EDGE_R = 0.8
TAB_ROOT_R = 1.5
ROD_ROOT_R = 0.3

VIEW = {"azimuth": 45, "elevation": 26}


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))



# ---------------- main L-shaped body (plan), without the end cap ----------------
body = (cq.Workplane("XY")
        .moveTo(NARROW_X0, CAP_L).lineTo(W, CAP_L).lineTo(W, L).lineTo(0, L)
        .lineTo(0, WIDE_Y0 - CORNER_RY * math.sin(math.radians(CORNER_END_ANG)))
        .ellipseArc(CORNER_RX, CORNER_RY, 180, CORNER_END_ANG, startAtCurrent=True)
        .lineTo(NARROW_X0, WIDE_Y0).close()
        .extrude(H))
body = body.edges("|Y").edges(cq.selectors.BoxSelector((-1, WIDE_Y0 - 1, -1), (1, L + 1, H + 1))).fillet(EDGE_R)

# ---------------- end cap with tapering rounds on its outer corners ----------------
cap = box(NARROW_X0, W, 0, CAP_L, 0, H).cut(
    box(NARROW_X0 - 1, W - WEB_T, -1, CAP_L + 1, LIP_T, H - LIP_T)).val()
mf = BRepFilletAPI_MakeFillet(cap.wrapped)
for e in cap.Edges():
    c = e.Center()
    p0 = e.startPoint()
    on_tb = abs(c.z - H) < 1e-6 or abs(c.z) < 1e-6
    if LIP_BLEND_R > 0 and on_tb and abs(c.x - NARROW_X0) < 1e-6 and abs(c.y - CAP_L / 2) < 1e-6:
        r_a, r_b = ((LIP_BLEND_R, BLEND_END_R) if p0.y < CAP_L / 2
                    else (BLEND_END_R, LIP_BLEND_R))
        mf.Add(r_a, r_b, e.wrapped)
    elif END_BLEND_R > 0 and on_tb and abs(c.y) < 1e-6:
        r_a, r_b = ((END_BLEND_R, BLEND_END_R) if p0.x < c.x
                    else (BLEND_END_R, END_BLEND_R))
        mf.Add(r_a, r_b, e.wrapped)
    elif (TIP_BLEND_R > 0 and abs(c.y) < 1e-6 and abs(c.x - NARROW_X0) < 1e-6
          and (c.z < LIP_T or c.z > H - LIP_T)):
        mf.Add(TIP_BLEND_R, e.wrapped)
mf.Build()
cap = cq.Workplane("XY").add(cq.Shape.cast(mf.Shape()))
body = body.union(cap)

# ---------------- channel: opening through the end cap ----------------
body = body.cut(box(NARROW_X0 - 1, W - WEB_T, -1, WIDE_Y0, LIP_T, H - LIP_T))

# deeper cavity behind the cap. In plan the cap's back face runs at
# CAP_BACK, swelling out with a concave round to CAP_BACK_TIP at the lip tips;
# it blends down into the thin flanges with a round that is large at the tips.
x0c, xw = NARROW_X0 - 1, W - WEB_T
arc_r = ((NARROW_X0 - CAP_BACK_X) ** 2 + (CAP_BACK_TIP - CAP_BACK) ** 2) / (2 * (CAP_BACK_TIP - CAP_BACK))
arc_cy = CAP_BACK + arc_r
y_x0c = arc_cy - math.sqrt(arc_r ** 2 - (x0c - CAP_BACK_X) ** 2)
xm = (x0c + CAP_BACK_X) / 2
ym = arc_cy - math.sqrt(arc_r ** 2 - (xm - CAP_BACK_X) ** 2)
cav = (cq.Workplane("XY").workplane(offset=FLANGE_T)
       .moveTo(x0c, WIDE_Y0).lineTo(x0c, y_x0c)
       .threePointArc((xm, ym), (CAP_BACK_X, CAP_BACK))
       .lineTo(xw, CAP_BACK).lineTo(xw, WIDE_Y0).close()
       .extrude(H - 2 * FLANGE_T))
cav_s = cav.val()
mf = BRepFilletAPI_MakeFillet(cav_s.wrapped)
for e in cav_s.Edges():
    c = e.Center()
    if not (abs(c.z - FLANGE_T) < 1e-6 or abs(c.z - (H - FLANGE_T)) < 1e-6):
        continue
    if c.y > CAP_BACK_TIP + 2:
        continue
    if e.geomType() == "CIRCLE":
        p0 = e.startPoint()
        r_a, r_b = ((CAP_BLEND_TIP_R, CAP_BLEND_R) if p0.x < c.x
                    else (CAP_BLEND_R, CAP_BLEND_TIP_R))
        mf.Add(r_a, r_b, e.wrapped)
    elif abs(c.y - CAP_BACK) < 1e-6:
        mf.Add(CAP_BLEND_R, e.wrapped)
mf.Build()
cav = cq.Workplane("XY").add(cq.Shape.cast(mf.Shape()))
body = body.cut(cav)


# ---------------- pipe notch and strap channel ----------------
cx, cy = W / 2, L
notch = cq.Workplane("XY").center(cx, cy).circle(NOTCH_R).extrude(H)
strap_ro = math.hypot(W / 2, L - WIN_Y0)
strap = (cq.Workplane("XY").workplane(offset=WIN_Z0)
         .center(cx, cy).circle(strap_ro).circle(STRAP_RI)
         .extrude(WIN_Z1 - WIN_Z0))
strap = strap.intersect(box(-5, W + 5, 0, L - STRAP_SKIN, WIN_Z0, WIN_Z1))
body = body.cut(notch).cut(strap)

# ---------------- screw holes through the web ----------------
for y in HOLE_Y:
    for z in (HOLE_Z_OFF, H - HOLE_Z_OFF):
        h = (cq.Workplane("YZ").workplane(offset=W - WEB_T - 0.5)
             .center(y, z).circle(HOLE_D / 2).extrude(WEB_T + 1))
        body = body.cut(h)

# ---------------- snap nubs (top and bottom) ----------------
zc_top = H + NUB_RISE - NUB_R
bead = (cq.Workplane("XZ").workplane(offset=-NUB_Y0)
        .center(NUB_X, zc_top).circle(NUB_R).extrude(-(NUB_Y1 - NUB_Y0)))
bead = bead.intersect(box(NUB_X - NUB_REACH, NUB_X + NUB_R + 1, NUB_Y0, NUB_Y1,
                          H - NUB_HANG, H + NUB_RISE + 1))
try:
    bead = bead.faces("<Y or >Y").edges("%CIRCLE").fillet(NUB_END_R)
except Exception:
    pass
# triangular hole running through the bead, under its -X overhang
tri = (cq.Workplane("XZ").workplane(offset=-(NUB_Y0 - 1))
       .polyline([(NUB_SLOT_X0, H - NUB_HANG + 0.3), (NUB_SLOT_X0, H),
                  (NARROW_X0 - 0.1, H)]).close()
       .extrude(-(NUB_Y1 - NUB_Y0 + 2)))
bead = bead.cut(tri)
bead_bot = bead.mirror("XY", basePointVector=(0, 0, H / 2))
body = body.union(bead).union(bead_bot)
# concave blend where the beads sit on the top / bottom faces (+X side)
bead_base = [e for e in body.edges().vals()
             if (abs(e.Center().z - H) < 1e-3 or abs(e.Center().z) < 1e-3)
             and e.Center().x > NUB_X and NUB_Y0 - 0.5 < e.Center().y < NUB_Y1 + 0.5
             and not (e.geomType() == "LINE" and abs(e.tangentAt(0.5).y) < 0.5)]
try:
    blended = body.val().fillet(NUB_BASE_R, bead_base)
    if blended.isValid():
        body = cq.Workplane("XY").add(blended)
except Exception:
    pass

# ---------------- hanging tab ----------------
dx, dy = TAB_P1[0] - TAB_P0[0], TAB_P1[1] - TAB_P0[1]
tab_len = math.hypot(dx, dy)
ang = math.degrees(math.atan2(dy, dx))
web = box(0, tab_len, -TAB_T / 2, TAB_T / 2, -TAB_DEPTH, 0.0)
web = web.edges("|Y and <Z and >X").fillet(TAB_CORNER_R)
try:
    # round over the free (bottom and far) edges of the web
    web = web.faces("<Y or >Y").edges(cq.selectors.BoxSelector(
        (0.5, -5, -TAB_DEPTH - 1), (tab_len + 1, 5, -0.3))).fillet(TAB_EDGE_R)
except Exception:
    pass
web = (web.rotate((0, 0, 0), (0, 0, 1), ang)
       .translate((TAB_P0[0], TAB_P0[1], 0)))
rod = (cq.Workplane("XY").workplane(offset=-TAB_DEPTH + ROD_R)
       .center(*TAB_P0).circle(ROD_R).extrude(TAB_DEPTH - ROD_R))
rod = rod.union(cq.Workplane("XY").sphere(ROD_R)
                .translate((TAB_P0[0], TAB_P0[1], -TAB_DEPTH + ROD_R)))
tab = web.union(rod)

# concave root blends where the tab meets the channel underside
s2 = math.sqrt(0.5)
for side in (1, -1):
    yo = side * TAB_T / 2
    root = (cq.Workplane("YZ")
            .moveTo(yo, 0).lineTo(yo + side * TAB_ROOT_R, 0)
            .threePointArc((yo + side * TAB_ROOT_R * (1 - s2), -TAB_ROOT_R * (1 - s2)),
                           (yo, -TAB_ROOT_R))
            .close().extrude(tab_len - TAB_CORNER_R - ROD_R)
            .translate((ROD_R, 0, 0))
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate((TAB_P0[0], TAB_P0[1], 0)))
    tab = tab.union(root)
rod_root = (cq.Workplane("XZ")
            .moveTo(ROD_R, 0).lineTo(ROD_R + ROD_ROOT_R, 0)
            .threePointArc((ROD_R + ROD_ROOT_R * (1 - s2), -ROD_ROOT_R * (1 - s2)),
                           (ROD_R, -ROD_ROOT_R))
            .close().revolve(360, (0, 0, 0), (0, 1, 0))
            .translate((TAB_P0[0], TAB_P0[1], 0)))
tab = tab.union(rod_root)
body = body.union(tab)

# hand back the single finished solid
solids = body.solids().vals()
result = cq.Workplane("XY").add(max(solids, key=lambda sh: sh.Volume()))
